import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Stamp block: rectangular base with a raised, mirrored emblem on top.
# The emblem is a disc split into a crescent (carrying the engraved, mirrored
# number "687") and an aircraft-nose motif (cabin windows, hull with a fin and
# a porthole, chin panel) separated by thin grooves cut down to the block top.
# ---------------------------------------------------------------------------

# Base block
BLOCK_L = 60.0      # X
BLOCK_W = 40.0      # Y
BLOCK_H = 20.0      # Z

# Raised emblem
RELIEF = 2.5                 # height of the relief above the block top
DISC_C = (0.2, 0.0)          # emblem disc centre
DISC_R = 18.8                # emblem disc radius
GAP = 0.65                   # width of the thin separating grooves

# crescent = disc minus an (inclined) elliptic "inner" region
ELL_C = (-14.95, -2.42)
ELL_A = 15.64                # semi-axis along ELL_ROT
ELL_B = 17.37
ELL_ROT = 41.66              # deg

# hull (capsule body, lower-left)
HULL_TOP = ((-20.0, -2.24), (3.0, -2.55))    # slightly inclined top edge
FIN_X0, FIN_X1 = -17.0, -15.15
FIN_TIP = (-16.15, 0.67)
HOLE_C = (-6.27, -6.5)
HOLE_D = 3.45
HULL_BOT_Y = -10.55

# chin panel (lower triangle) and the V-groove around it
CHIN_TOP_Y = -11.2
CHIN_C = (-13.5, -4.0)
CHIN_R = 12.6

# cabin windows
WIN_Y = 7.3
LW_X = -14.6                 # right edge of the left (triangular) window
MW_X = -13.8                 # left edge of the middle window
MW_A = 4.67
MW_B = 5.2
RW_GAP_L = 0.75              # gap middle -> right window
RW_C = (-13.35, 1.65)        # right window: outer (right) edge arc
RW_R = 10.96
MW_FILLET = 0.5              # rounded top corner of the middle window

# wing-shaped notch in the crescent horn
NOTCH_Y = 13.5
NOTCH_HW = 0.62
NOTCH_TIP_X = -0.35

Z0 = BLOCK_H            # relief floor (block top)
BIG = 80.0


def wp(z=Z0):
    return cq.Workplane("XY").workplane(offset=z)


def cyl(c, r, h=RELIEF):
    return wp().center(*c).circle(r).extrude(h)


def box(x0, x1, y0, y1, h=RELIEF):
    return wp().center((x0 + x1) / 2, (y0 + y1) / 2).rect(x1 - x0, y1 - y0).extrude(h)


def poly(pts, h=RELIEF):
    return wp().polyline(pts).close().extrude(h)


def ell(c, a, b, rot=0.0, h=RELIEF):
    return wp().center(*c).ellipse(a, b, rot).extrude(h)


def hull_y(x):
    (x0, y0), (x1, y1) = HULL_TOP
    return y0 + (y1 - y0) * (x - x0) / (x1 - x0)


# ---------------------------------------------------------------- base block
block = cq.Workplane("XY").box(BLOCK_L, BLOCK_W, BLOCK_H, centered=(True, True, False))

disc = cyl(DISC_C, DISC_R)
inner = ell(ELL_C, ELL_A, ELL_B, ELL_ROT)
inner_g = ell(ELL_C, ELL_A - GAP, ELL_B - GAP, ELL_ROT)          # inner, shrunk by GAP

# ---------------------------------------------------------------- crescent
crescent = disc.cut(inner)

# one smooth spline outline: full width on the left, rounded tip on the right
nx = NOTCH_TIP_X
notch = (wp().moveTo(-16.0, NOTCH_Y + NOTCH_HW)
         .spline([(nx - 8.0, NOTCH_Y + NOTCH_HW),
                  (nx - 3.0, NOTCH_Y + 0.75 * NOTCH_HW),
                  (nx, NOTCH_Y),
                  (nx - 3.0, NOTCH_Y - 0.75 * NOTCH_HW),
                  (nx - 8.0, NOTCH_Y - NOTCH_HW),
                  (-16.0, NOTCH_Y - NOTCH_HW)], includeCurrent=True)
         .close().extrude(RELIEF))
crescent = crescent.cut(notch)

# ---------------------------------------------------------------- mirrored "687"
DIG_TOP = 4.68
DIG_BOT = -1.45

# "7" (mirrored): bar with a rounded end + diagonal stroke
seven = (wp().moveTo(2.63, DIG_TOP)
         .lineTo(5.98, DIG_TOP)
         .threePointArc((6.54, 4.12), (5.98, 3.56))
         .lineTo(4.22, 3.56)
         .lineTo(6.9, DIG_BOT)
         .lineTo(5.95, DIG_BOT)
         .lineTo(2.63, 4.25)
         .close().extrude(RELIEF))

# "8": two stacked bowls with counters
eight = (ell((9.52, 3.3), 1.7, 1.4)
         .union(ell((9.52, 0.4), 2.02, 1.83))
         .cut(ell((9.47, 3.08), 0.62, 0.66))
         .cut(ell((9.62, 0.40), 0.84, 0.76)))

# "6" (mirrored): bowl + curved tail
bowl6 = ell((14.32, 0.55), 1.98, 1.98).cut(ell((14.38, 0.6), 0.78, 0.9))
tail_c = (13.3, 1.27)
tail = (cyl(tail_c, 3.42).cut(cyl(tail_c, 2.45))
        .intersect(box(12.1, 16.4, 1.3, 6.0)))
six = bowl6.union(tail)

crescent = crescent.cut(seven.union(eight).union(six))

# ---------------------------------------------------------------- hull
(hx0, hy0), (hx1, hy1) = HULL_TOP
hull = (disc.intersect(inner_g)
        .intersect(poly([(hx0, hy0), (hx1, hy1), (hx1, -BIG / 2), (hx0, -BIG / 2)])))
# V-groove around the chin panel
hull = hull.cut(cyl(CHIN_C, CHIN_R + GAP).intersect(box(-BIG, BIG, -BIG, HULL_BOT_Y)))
# fin
fin = poly([(FIN_X0, hull_y(FIN_X0)), FIN_TIP, (FIN_X1, hull_y(FIN_X1)),
            (FIN_X1, hull_y(FIN_X1) - 0.5), (FIN_X0, hull_y(FIN_X0) - 0.5)])
hull = hull.union(fin)
# porthole
hull = hull.cut(cyl(HOLE_C, HOLE_D / 2))

# ---------------------------------------------------------------- chin panel
chin = (disc.intersect(cyl(CHIN_C, CHIN_R))
        .intersect(box(-BIG, BIG, -BIG, CHIN_TOP_Y)))

# ---------------------------------------------------------------- windows
lw = disc.intersect(box(-BIG, LW_X, WIN_Y, BIG))
mw = (disc.intersect(ell((MW_X, WIN_Y), MW_A, MW_B))
      .intersect(box(MW_X, BIG, WIN_Y, BIG)))
mw = mw.edges(cq.selectors.NearestToPointSelector((MW_X, WIN_Y + MW_B, Z0 + RELIEF / 2))).fillet(MW_FILLET)
rw = (cyl(RW_C, RW_R).intersect(box(MW_X, BIG, WIN_Y, BIG))
      .cut(ell((MW_X, WIN_Y), MW_A + RW_GAP_L, MW_B + RW_GAP_L)))

# ---------------------------------------------------------------- assemble
relief = crescent.union(hull).union(chin).union(lw).union(mw).union(rw)
result = block.union(relief)

VIEW = {"azimuth": 45, "elevation": 26}
